import cadquery as cq

# ---------------------------------------------------------------
# One-octave piano keyboard (7 white keys + 5 black keys)
# X: across the keyboard (C at x=0), Y: along the keys (front at y=0),
# Z: up (key bottoms at z=0)
# ---------------------------------------------------------------

# --- overall key dimensions (mm) ---
H = 8.75            # white key / lever thickness
W_FRONT = 20.0      # white key front width
L_FRONT = 34.8      # length of the wide front part of white keys
Y_STEP = 97.2       # end of full-width key body (neck starts)
Y_FL0 = 122.8       # flange start
Y_FL1 = 125.6       # flange end / tab start
Y_END = 131.9       # tab end
NECK_INSET = 0.5    # neck side inset
TAB_W = 3.5         # tab width

# V notch on the underside of every key tail
NOTCH_Y = 109.8
NOTCH_HALF = 4.0
NOTCH_DEPTH = 4.1

# --- black keys ---
BK_W = 11.2         # black key base width (= lever width)
BK_TOP_W = 8.5      # black key top width
BK_H = 8.75         # height of the black key block above the levers
BK_Y0 = 36.95       # black key front (base)
BK_FRONT_SLOPE = 1.9  # set-back of the top front edge
BK_Y1 = 87.25       # black key back end

# --- underside hollowing ---
WALL = 2.5
TOP_SKIN = 2.6
CAV_END = 102.5     # cavities stop just ahead of the pivot notch

# white keys: (front left x, back-section left x, back-section right x,
#              small fore/aft placement offset of the key, + = towards the front)
WHITE = [
    (0.0,   0.0,   10.8,  0.42),   # C
    (23.9,  26.9,  40.0,  0.97),   # D
    (47.5,  56.6,  67.5,  0.83),   # E
    (70.0,  70.0,  81.0, -0.16),   # F
    (93.1,  96.4, 106.7, -0.41),   # G
    (116.3, 122.1, 132.4, -0.71),  # A
    (139.5, 148.6, 159.5, -0.87),  # B
]
# black keys: (centre x, fore/aft placement offset)
BLACK = [(18.74, 0.0), (47.45, 0.0), (88.5, 0.07), (114.7, 0.02), (140.25, -0.42)]


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def tail(x0, x1):
    """neck + flange + tab for a key whose back section spans x0..x1"""
    xc = 0.5 * (x0 + x1)
    t = box(x0 + NECK_INSET, x1 - NECK_INSET, Y_STEP - 0.01, Y_FL0 + 0.01, 0, H)
    t = t.union(box(x0, x1, Y_FL0, Y_FL1 + 0.01, 0, H))
    t = t.union(box(xc - TAB_W / 2, xc + TAB_W / 2, Y_FL1, Y_END, 0, H))
    return t


def notch_cutter(x0, x1):
    prof = (cq.Workplane("YZ", origin=(x0 - 1, 0, 0))
            .polyline([(NOTCH_Y - NOTCH_HALF, -0.01),
                       (NOTCH_Y, NOTCH_DEPTH),
                       (NOTCH_Y + NOTCH_HALF, -0.01)])
            .close()
            .extrude(x1 - x0 + 2))
    return prof


def pocket(pts, x0, x1):
    """underside cavity: the key outline offset inwards by the wall
    thickness (rounded at inside corners), open at the bottom and
    closed at the back just ahead of the pivot notch"""
    cav = (cq.Workplane("XY", origin=(0, 0, -1))
           .polyline(pts).close()
           .offset2D(-WALL, "arc")
           .extrude(H - TOP_SKIN + 1))
    return cav.cut(box(x0 - 1, x1 + 1, CAV_END, Y_END + 1, -2, H))


def white_key(xf, xb0, xb1):
    k = box(xf, xf + W_FRONT, 0, L_FRONT, 0, H)
    k = k.union(box(xb0, xb1, 0, Y_STEP, 0, H))
    k = k.union(tail(xb0, xb1))
    # hollow underside following the key outline
    n0, n1 = xb0 + NECK_INSET, xb1 - NECK_INSET
    pts = [(xf, 0), (xf + W_FRONT, 0), (xf + W_FRONT, L_FRONT), (xb1, L_FRONT),
           (xb1, Y_STEP), (n1, Y_STEP), (n1, Y_FL0), (n0, Y_FL0),
           (n0, Y_STEP), (xb0, Y_STEP), (xb0, L_FRONT), (xf, L_FRONT)]
    # drop duplicate points where the back section is flush with the front
    clean = []
    for p in pts:
        if not clean or (abs(p[0] - clean[-1][0]) > 1e-6 or abs(p[1] - clean[-1][1]) > 1e-6):
            clean.append(p)
    # remove collinear points
    out = []
    n = len(clean)
    for i in range(n):
        a, b, c = clean[i - 1], clean[i], clean[(i + 1) % n]
        cross = (b[0] - a[0]) * (c[1] - b[1]) - (b[1] - a[1]) * (c[0] - b[0])
        if abs(cross) > 1e-9:
            out.append(b)
    k = k.cut(pocket(out, xf, xf + W_FRONT))
    k = k.cut(notch_cutter(xb0, xb1))
    return k


def black_key(xc):
    x0, x1 = xc - BK_W / 2, xc + BK_W / 2
    lever = box(x0, x1, BK_Y0, Y_STEP, 0, H)
    lever = lever.union(tail(x0, x1))
    # raised block (tapered sides, sloped front, vertical back)
    base = (cq.Workplane("XY", origin=(0, 0, H))
            .polyline([(x0, BK_Y0), (x1, BK_Y0), (x1, BK_Y1), (x0, BK_Y1)]).close())
    ti = (BK_W - BK_TOP_W) / 2
    top = (cq.Workplane("XY", origin=(0, 0, H + BK_H))
           .polyline([(x0 + ti, BK_Y0 + BK_FRONT_SLOPE), (x1 - ti, BK_Y0 + BK_FRONT_SLOPE),
                      (x1 - ti, BK_Y1), (x0 + ti, BK_Y1)]).close())
    blk = cq.Solid.makeLoft([base.wires().val(), top.wires().val()], True)
    k = lever.union(cq.Workplane("XY").add(blk))
    n0, n1 = x0 + NECK_INSET, x1 - NECK_INSET
    k = k.cut(pocket([(x0, BK_Y0), (x1, BK_Y0), (x1, Y_STEP), (n1, Y_STEP),
                      (n1, Y_FL0), (n0, Y_FL0), (n0, Y_STEP), (x0, Y_STEP)], x0, x1))
    k = k.cut(notch_cutter(x0, x1))
    return k


result = cq.Workplane("XY")
for (xf, xb0, xb1, dy) in WHITE:
    result = result.union(white_key(xf, xb0, xb1).translate((0, -dy, 0)))
for (xc, dy) in BLACK:
    result = result.union(black_key(xc).translate((0, -dy, 0)))
